import cadquery as cq

# =====================================================================
# Base plate with a stepped, hollow housing near the front-left corner.
# Square plate, chamfered corners, 4 counterbored corner holes (screw
# heads from below), a rectangular through-opening under the housing,
# and engraved lettering on the underside.
# Coordinates: plate centred on the origin, plate bottom at Z = 0.
# =====================================================================

# ---------------- plate ----------------
L = 300.0          # plate side (square)
T = 8.0            # plate thickness
CORNER_CH = 2.75   # 45 deg chamfer on the four vertical plate corners
HOLE_INSET = 12.0  # corner hole centre distance from each plate edge
HOLE_D = 4.0       # corner through-hole diameter
CB_D = 10.5        # counterbore diameter (underside)
CB_DEPTH = 5.0     # counterbore depth (underside)

# ---------------- housing ----------------
# extents measured from the plate's front-left corner (-X, -Y)
BX0, BX1 = 33.2, 97.3      # x extent of housing
BY0, BY1 = 32.8, 132.5     # y extent of housing
Y_STEP = 89.7              # y where the roofed (taller) rear section starts
H_LOW = 30.0               # height of the open front section above the plate
H_HIGH = 38.0              # height of the roofed rear section above the plate
WALL = 7.5                 # side / front wall thickness
WALL_BACK = 8.0            # rear wall thickness

# ---------------- underside lettering ----------------
# (text, font size, y of line centre) - reads correctly from below
TEXT_LINES = [("ECE 1896", 12.0, -51.5), ("Senior Design", 11.3, -35.6)]
TEXT_X = 10.5              # x of the text block centre
TEXT_DEPTH = 1.0           # engraving depth

# =====================================================================
# plate
plate = (
    cq.Workplane("XY")
    .rect(L, L)
    .extrude(T)
    .edges("|Z").chamfer(CORNER_CH)
)
hole_pts = [
    (sx * (L / 2 - HOLE_INSET), sy * (L / 2 - HOLE_INSET))
    for sx in (-1, 1) for sy in (-1, 1)
]
plate = (
    plate.faces("<Z").workplane()
    .pushPoints(hole_pts)
    .cboreHole(HOLE_D, CB_D, CB_DEPTH)
)

# housing coordinates -> plate-centred coordinates
x0, x1 = BX0 - L / 2, BX1 - L / 2
y0, y1 = BY0 - L / 2, BY1 - L / 2
ys = Y_STEP - L / 2
xm = (x0 + x1) / 2
bw = x1 - x0

# outer housing: low open front block + taller roofed rear block
front_blk = (
    cq.Workplane("XY").workplane(offset=T)
    .center(xm, (y0 + ys) / 2)
    .rect(bw, ys - y0).extrude(H_LOW)
)
rear_blk = (
    cq.Workplane("XY").workplane(offset=T)
    .center(xm, (ys + y1) / 2)
    .rect(bw, y1 - ys).extrude(H_HIGH)
)
body = plate.union(front_blk).union(rear_blk)

# inner cavity: runs through the plate up to the front-section top,
# covered by the roof of the rear section
cx0, cx1 = x0 + WALL, x1 - WALL
cy0, cy1 = y0 + WALL, y1 - WALL_BACK
cavity = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .center((cx0 + cx1) / 2, (cy0 + cy1) / 2)
    .rect(cx1 - cx0, cy1 - cy0)
    .extrude(T + H_LOW + 1.0)
)
# open top of the front section (from the front wall back to the step)
opening = (
    cq.Workplane("XY").workplane(offset=T)
    .center((cx0 + cx1) / 2, (cy0 + ys) / 2)
    .rect(cx1 - cx0, ys - cy0)
    .extrude(H_LOW + 1.0)
)
body = body.cut(cavity).cut(opening)

# underside engraving (plane normal -Z, x along +X: readable from below)
for txt, size, y in TEXT_LINES:
    try:
        under = cq.Plane(origin=(TEXT_X, y, 0.0), xDir=(1, 0, 0),
                         normal=(0, 0, -1))
        letters = cq.Workplane(under).text(
            txt, size, -TEXT_DEPTH, combine=False, kind="bold",
            halign="center", valign="center",
        )
        engraved = body.cut(letters)
        if engraved.val().isValid():
            body = engraved
    except Exception:
        pass  # lettering is cosmetic; keep the plain part if fonts fail

result = body

VIEW = {"azimuth": 45, "elevation": 26}
